import math
import cadquery as cq

# =====================================================================
# Fan grill / fan mount block with honeycomb grill, bottom channel and
# flared feet.  Origin: centre of the fan hole pattern, Z=0 at the bottom.
# =====================================================================

# ---------------- driving dimensions (mm) ----------------
W = 68.7            # X width of body
Y_POS = 35.9        # +Y face position
Y_NEG = -35.05      # -Y face position (top, below the bevel)
Y_NEG_BOT = -36.6   # -Y face position at the bottom (drafted face)
H = 20.4            # overall height

# vertical corner cuts, given by their legs along the Y faces (in X) and
# along the X faces (in Y)
CP_X, CP_Y = 4.15, 5.2      # +Y corners
CN_X, CN_Y = 3.65, 3.65     # -Y corners

# top edge bevel (horizontal inset per edge, common height)
BEV_H = 1.7
BEV_X = 1.6         # +/-X edges and corner cuts
BEV_YP = 1.1        # +Y edge
BEV_YN = 2.0        # -Y edge

# feet (flared pads on the +/-Y faces near each corner)
FOOT_YP = 39.8          # +Y feet outer face
FOOT_YN = -40.5         # -Y feet outer face
FOOT_ZP = 7.9           # +Y feet: top of the vertical outer face (corner side)
FOOT_ZN = 5.8           # -Y feet: top of the vertical outer face (corner side)
FOOT_ZIN_P = 16.8       # +Y feet: flare leaves the face on the inner side
FOOT_ZIN_N = 14.5       # -Y feet: flare leaves the face on the inner side
FOOT_IN_P = (20.0, 37.0)        # +Y inner side face: outer point |X|, angle to X (deg)
FOOT_XA_N = 14.3                # -Y inner face: |X| where it leaves the face at the top
FOOT_B_N = (22.5, 2.9)          # -Y inner face: |X|, Z at the outer face bottom
FOOT_C_N = (15.3, Y_NEG_BOT)    # -Y inner face: |X|, Y at Z = 0
FOOT_CH_Z = 2.9         # -Y feet bottom chamfer height
FOOT_CH_Y = Y_NEG_BOT   # -Y feet bottom chamfer foot line

# bottom channel along X
CH_Y = -1.23        # channel centre line
CH_BOT = 24.56      # half width at bottom
CH_TOP = 13.28      # half width at ceiling
CH_H = 8.28         # channel height

# top edge notches on the +/-X edges
GR_Y = -1.23        # notch centre
GR_X = 2.8          # horizontal size of the notch slope
GR_Z = 4.2          # vertical size of the notch slope
GR_HW_TOP = 13.2    # half length of the notch on the top face
GR_HW_MID = 14.3    # half width at the side face, bevel level
GR_HW_BOT = 13.1    # half width at the side face, notch bottom

# fan pocket from below
POCKET = 62.5
POCKET_R = 7.0
PLATE = 5.8         # top plate thickness over the pocket

# honeycomb grill
GRILL_D = 60.3      # clip circle of the hexagons
BORE_D = 61.5       # bore below the grill
GRILL_T = 1.6
HEX_PITCH = 7.7     # centre distance of neighbouring cells
HEX_FLAT = 6.35     # hole size across flats

# mounting holes
HOLE_SP = 50.0
HOLE_D = 5.0
CB_D = 8.3
CB_DEPTH = 3.0
CB_CH = 0.65
SQ = 5.4            # printing bridge square under the counterbore
SQ_DEPTH = 0.5


# ---------------- helpers ----------------
def halfspace(p, n, size=400.0):
    """Solid occupying {x : (x - p) . n >= 0} (clipped to a big box)."""
    n = cq.Vector(*n).normalized()
    ref = cq.Vector(0, 0, 1) if abs(n.z) < 0.9 else cq.Vector(1, 0, 0)
    xd = ref.cross(n).normalized()
    pl = cq.Plane(origin=cq.Vector(*p), xDir=xd, normal=n)
    return cq.Workplane(pl).rect(size, size).extrude(size).val()


def plane_from_pts(a, b, c):
    a, b, c = cq.Vector(*a), cq.Vector(*b), cq.Vector(*c)
    return a, (b - a).cross(c - a).normalized()


def offset_polygon(pts, offs):
    """Inset a convex CCW polygon, edge i (pts[i]->pts[i+1]) by offs[i]."""
    n = len(pts)
    lines = []
    for i in range(n):
        (x0, y0), (x1, y1) = pts[i], pts[(i + 1) % n]
        dx, dy = x1 - x0, y1 - y0
        L = math.hypot(dx, dy)
        nx, ny = -dy / L, dx / L          # inward normal for CCW
        lines.append(((x0 + nx * offs[i], y0 + ny * offs[i]), (dx, dy)))
    out = []
    for i in range(n):
        (p, d), (q, e) = lines[i - 1], lines[i]
        den = d[0] * e[1] - d[1] * e[0]
        t = ((q[0] - p[0]) * e[1] - (q[1] - p[1]) * e[0]) / den
        out.append((p[0] + d[0] * t, p[1] + d[1] * t))
    return out


hx = W / 2


def corner_x(y, side):
    """|X| of the vertical corner cut plane at a given Y (side = +1 / -1)."""
    if side > 0:
        return hx - CP_X * (y - (Y_POS - CP_Y)) / CP_Y
    return hx - CN_X * ((Y_NEG + CN_Y) - y) / CN_Y


def corner_halfspace(side):
    """Half space beyond the corner cut on the +X side."""
    if side > 0:
        return halfspace((hx, Y_POS - CP_Y, 0), (CP_Y, CP_X, 0))
    return halfspace((hx, Y_NEG + CN_Y, 0), (CN_Y, -CN_X, 0))


# ---------------- body with bevelled top ----------------
def outline_at(yneg):
    """Body outline (CCW) with the -Y face at yneg."""
    xn = corner_x(yneg, -1)
    return [
        (-xn, yneg), (xn, yneg),
        (hx, Y_NEG + CN_Y), (hx, Y_POS - CP_Y),
        (hx - CP_X, Y_POS), (-(hx - CP_X), Y_POS),
        (-hx, Y_POS - CP_Y), (-hx, Y_NEG + CN_Y),
    ]


def poly_wire(pts, z):
    return cq.Wire.makePolygon([cq.Vector(x, y, z) for x, y in pts], close=True)


outline = outline_at(Y_NEG)
bottom = outline_at(Y_NEG_BOT)
offs = [BEV_YN, BEV_X, BEV_X, BEV_X, BEV_YP, BEV_X, BEV_X, BEV_X]
inset = offset_polygon(outline, offs)

lower = cq.Solid.makeLoft([poly_wire(bottom, 0.0), poly_wire(outline, H - BEV_H)], True)
cap = cq.Solid.makeLoft([poly_wire(outline, H - BEV_H), poly_wire(inset, H)], True)
body = cq.Workplane().add(lower).union(cq.Workplane().add(cap)).clean()


# ---------------- feet ----------------
def foot(sx, side):
    """One flared foot, built on the +X side and mirrored for -X."""
    if side > 0:
        yf, yo = Y_POS, FOOT_YP
        xo, ang = FOOT_IN_P
        t = math.tan(math.radians(ang))
        x_in = xo - (yo - yf) / t
        p1 = (corner_x(yf, 1), yf, H - BEV_H)   # flare start at the corner
        p2 = (x_in, yf, FOOT_ZIN_P)             # flare start on the inner side
        p3 = (corner_x(yo, 1), yo, FOOT_ZP)     # outer face top at the corner
        blk = cq.Workplane("XY").box(hx, 11, H - BEV_H, centered=False).translate((0, yf - 1, 0)).val()
    else:
        yf, yo = Y_NEG, FOOT_YN
        p1 = (corner_x(yf, -1), yf, H - BEV_H)
        y2 = Y_NEG + (Y_NEG_BOT - Y_NEG) * (H - BEV_H - FOOT_ZIN_N) / (H - BEV_H)
        p2 = (FOOT_XA_N, y2, FOOT_ZIN_N)
        p3 = (corner_x(yo, -1), yo, FOOT_ZN)
        blk = cq.Workplane("XY").box(hx, 11, H - BEV_H, centered=False).translate((0, yf - 10, 0)).val()
    sp, sn = plane_from_pts(p1, p2, p3)
    if sn.y * side < 0:                      # normal away from the body
        sn = -sn
    f = blk.cut(halfspace(sp, sn))                         # flared face
    f = f.cut(halfspace((0, yo, 0), (0, side, 0)))         # outer face
    if side > 0:
        nin = cq.Vector(-math.sin(math.radians(ang)), math.cos(math.radians(ang)), 0)
        f = f.cut(halfspace((xo, yo, 0), nin))             # inner side face
        f = f.cut(corner_halfspace(1))                     # corner cut
    else:
        b = (FOOT_B_N[0], yo, FOOT_B_N[1])
        c = (FOOT_C_N[0], FOOT_C_N[1], 0.0)
        tp, tn = plane_from_pts(p2, b, c)
        if tn.x > 0:
            tn = -tn
        f = f.cut(halfspace(tp, tn))                       # inner side face
        f = f.cut(corner_halfspace(-1))                    # corner cut
        f = f.cut(halfspace((0, FOOT_YN, FOOT_CH_Z),       # bottom chamfer
                            (0, -1.0, -(FOOT_CH_Y - FOOT_YN) / FOOT_CH_Z)))
    wp = cq.Workplane().add(f)
    if sx < 0:
        wp = wp.mirror("YZ")
    return wp


for sx in (1, -1):
    for side in (1, -1):
        body = body.union(foot(sx, side))

# ---------------- bottom channel (through along X) ----------------
chan = (
    cq.Workplane("YZ", origin=(-W, CH_Y, 0))
    .polyline([(-CH_BOT - 1, -1), (CH_BOT + 1, -1), (CH_BOT, 0), (CH_TOP, CH_H),
               (-CH_TOP, CH_H), (-CH_BOT, 0)]).close()
    .extrude(2 * W)
)
body = body.cut(chan)

# ---------------- top notches on the +/-X edges ----------------
for sx in (1, -1):
    # sloped notch face from (hx - GR_X, H) down to (hx, H - GR_Z)
    n_sl = cq.Vector(GR_Z, 0, GR_X).normalized()
    g = cq.Workplane("XY").box(GR_X + 6, 2 * GR_HW_MID + 6, GR_Z + 6).translate((hx, GR_Y, H)).val()
    g = g.intersect(halfspace((hx - GR_X, GR_Y, H), n_sl))
    # inclined end walls of the notch
    for sy in (1, -1):
        p1 = (hx - GR_X, GR_Y + sy * GR_HW_TOP, H)
        p2 = (hx, GR_Y + sy * GR_HW_BOT, H - GR_Z)
        p3 = (hx, GR_Y + sy * GR_HW_MID, H - BEV_H)
        pp, nn = plane_from_pts(p1, p2, p3)
        if nn.y * sy < 0:
            nn = -nn
        g = g.cut(halfspace(pp, nn))
    wp = cq.Workplane().add(g)
    if sx < 0:
        wp = wp.mirror("YZ")
    body = body.cut(wp)

# ---------------- fan pocket from below ----------------
pocket = (
    cq.Workplane("XY")
    .rect(POCKET, POCKET)
    .extrude(H - PLATE)
    .edges("|Z")
    .fillet(POCKET_R)
)
body = body.cut(pocket)
bore = (cq.Workplane("XY", origin=(0, 0, H - PLATE - 0.5))
        .circle(BORE_D / 2).extrude(PLATE + 0.5 - GRILL_T))
body = body.cut(bore)

# ---------------- honeycomb grill ----------------
col = HEX_PITCH * math.sqrt(3) / 2
pts = []
n = int(GRILL_D / col) + 2
for i in range(-n, n + 1):
    for j in range(-n, n + 1):
        x = i * col
        y = j * HEX_PITCH + (HEX_PITCH / 2 if i % 2 else 0.0)
        if math.hypot(x, y) < GRILL_D / 2 + HEX_PITCH:
            pts.append((x, y))
z0 = H - GRILL_T - 1
hexes = (
    cq.Workplane("XY", origin=(0, 0, z0))
    .pushPoints(pts)
    .polygon(6, HEX_FLAT * 2 / math.sqrt(3))
    .extrude(GRILL_T + 2)
)
disk = cq.Workplane("XY", origin=(0, 0, z0)).circle(GRILL_D / 2).extrude(GRILL_T + 2)
body = body.cut(hexes.intersect(disk))

# ---------------- mounting holes ----------------
hp = [(sx * HOLE_SP / 2, sy * HOLE_SP / 2) for sx in (1, -1) for sy in (1, -1)]
for (x, y) in hp:
    cb = cq.Workplane("XY", origin=(x, y, H - CB_DEPTH)).circle(CB_D / 2).extrude(CB_DEPTH + 1)
    cs = cq.Solid.makeCone(CB_D / 2, CB_D / 2 + CB_CH + 1.0, CB_CH + 1.0,
                           pnt=cq.Vector(x, y, H - CB_CH), dir=cq.Vector(0, 0, 1))
    sq = cq.Workplane("XY", origin=(x, y, H - CB_DEPTH - SQ_DEPTH)).rect(SQ, SQ).extrude(SQ_DEPTH + 0.1)
    th = cq.Workplane("XY", origin=(x, y, H - PLATE - 1)).circle(HOLE_D / 2).extrude(PLATE + 2)
    body = body.cut(cb).cut(cq.Workplane().add(cs)).cut(sq).cut(th)

result = body
